import cadquery as cq

# =====================================================================
#  Hinged tray / cover frame with a window, mounting tabs and posts
#  X = length, Y = width, Z = height.  Hinge knuckle end at +X.
# =====================================================================

# ---------------- overall ----------------
L = 120.0        # overall length (X)
W = 88.9         # overall width (Y)
H = 22.2         # overall height (Z)

# ---------------- outer shell ----------------
T_BASE = 1.6     # base plate thickness (= inner floor level)
LIP_W = 2.6      # -X bottom lip projection
LIP_H = 2.9      # -X bottom lip height
RAIL_W = 2.4     # side rail width (Y)
RAIL_H = 12.2    # side rail / -X lower block height
XBLK_W = 3.9     # -X lower block width (X)
WALL_T = 2.5     # side wall thickness
XWALL_T = 1.8    # -X wall thickness
END_R = 7.5      # rounded top edge radius at +X end

X_WALL0 = LIP_W + XBLK_W            # outer face of -X upper wall
X_IN = X_WALL0 + XWALL_T            # inner face of -X wall
YI0 = RAIL_W + WALL_T               # inner face of -Y wall
YI1 = W - RAIL_W - WALL_T           # inner face of +Y wall

# side rail taper into the rounded end plates
TAPER_X0 = 95.7                     # rail top ends here
TAPER_X1 = 106.2                    # rail taper meets base plate here

# ---------------- +X hinge end ----------------
BLK_X0 = 107.5   # back of hinge blocks / face of walls A and C
LEDGE_X = 109.9  # front edge of ledge behind channel
BLK_H = 14.1     # hinge block top height
LEDGE_DROP = 0.4
CH_FIL = 0.8     # fillet at foot of channel back wall
CH_Y0, CH_Y1 = 21.3, 67.8           # hinge channel between blocks
PIN_X, PIN_Z, PIN_D = 113.3, 9.6, 2.5

# zig-zag inner wall at +X end of the cavity
ZW_T = 2.1
WB_X0 = 99.9                        # wall B inner face
WA_X0 = 105.3                       # wall A inner face
WC_X0 = 104.9                       # wall C inner face
ZJ1_Y0, ZJ1_Y1 = 14.2, 16.8         # connector B-C
ZJ2_Y0, ZJ2_Y1 = 52.7, 55.4         # connector A-B
WB_FIL = 0.8                        # rounded top outer edge of wall B

# ---------------- bottom pad and window ----------------
PAD_X0, PAD_X1, PAD_Y0, PAD_Y1, PAD_T = 29.7, 104.0, 5.5, 68.9, 1.2
PAD_CH = 0.5
WIN_X0, WIN_X1, WIN_Y0, WIN_Y1 = 39.6, 94.8, 14.6, 59.8

# ---------------- -X wall opening ----------------
OP_Y0, OP_Y1, OP_Z0, OP_Z1 = 11.2, 61.5, T_BASE, 10.9

# ---------------- interior ramp / slopes / ribs ----------------
RAMP_H = 6.3     # ramp rib (wedge) on the -X side of the window
RAMP_X0 = 20.4
SLOPE_X1 = 24.4
SLOPE_ZB = 3.0
RIB_Y0, RIB_T, RIB_H = 60.6, 1.6, 8.2          # rib along +Y side of window
RIBN_Y0, RIBN_T, RIBN_X0, RIBN_X1 = 11.6, 1.8, 22.0, 101.4   # rib along -Y side
RIB_X0, RIB_X1 = 22.2, 62.1
SLOT_X0, SLOT_X1, SLOT_Y0, SLOT_W = 65.7, 103.0, 61.0, 1.5

# ---------------- tabs, posts, holes ----------------
TAB_Y0, TAB_T, TAB_H = 72.5, 2.1, 10.0
TABS = ((16.2, 26.4), (52.9, 63.1))
TAB_HOLE_Z, TAB_HOLE_D, TAB_PIN_D, TAB_PIN_DX = 5.9, 2.6, 1.2, 3.7
TAB_FIL = 0.8
POST_D, POST_H, POST_FIL, POST_HOLE = 4.6, 8.3, 1.0, 0.9
POSTS = ((40.7, 70.2), (66.7, 72.2), (93.2, 70.2))
SQ_HOLES = ((74.9, 71.4), (100.2, 71.4))
POST_THROUGH = 1
BOT_HOLES = ((35.0, 2.8), (66.3, 2.8), (94.9, 2.8))   # blind, from below
BOT_HOLE_D, BOT_HOLE_DEPTH = 0.9, 4.0
WALL_FIL = 1.2   # concave fillet between floor and +Y wall


# ---------------------------------------------------------------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def xz_prism(pts, y0, y1):
    """Prism from an XZ polygon, extruded from y0 to y1."""
    return (cq.Workplane("XZ").polyline(pts).close()
            .extrude(-(y1 - y0)).translate((0, y0, 0)))


def mirror_y(wp):
    return wp.mirror("XZ", (0, W / 2, 0))


# ---------------- base plate, lip, pad ----------------
body = box(0, L, 0, W, 0, T_BASE)
body = body.union(box(0, LIP_W + 0.01, 0, W, 0, LIP_H))
pad = (box(PAD_X0, PAD_X1, PAD_Y0, PAD_Y1, -PAD_T, 0.01)
       .faces("<Z").edges().chamfer(PAD_CH))
body = body.union(pad)

# -X lower block
body = body.union(box(LIP_W, X_WALL0, 0, W, 0, RAIL_H))

# ---------------- side rails with tapered +X end ----------------
rail = box(LIP_W, L, 0, RAIL_W, 0, RAIL_H)
rail = rail.cut(xz_prism([(TAPER_X0, RAIL_H + 1), (TAPER_X0, RAIL_H),
                          (TAPER_X1, T_BASE), (TAPER_X1, -1),
                          (L + 10, -1), (L + 10, RAIL_H + 1)], -1, RAIL_W + 1))
body = body.union(rail).union(mirror_y(rail))

# ---------------- perimeter walls ----------------


def side_wall(y0, y1):
    w = box(X_WALL0, L, y0, y1, 0, H)
    return w.edges("|Y and >X and >Z").fillet(END_R)


wall_s = side_wall(RAIL_W, RAIL_W + WALL_T)
body = body.union(wall_s).union(mirror_y(wall_s))
body = body.union(box(X_WALL0, X_IN, RAIL_W, W - RAIL_W, 0, H))

# ---------------- interior ramp rib and ribs around the window ----------------
# wedge-shaped ramp rib: vertical back face, sloped front towards window
ramp = xz_prism([(RAMP_X0, 0), (SLOPE_X1, 0), (SLOPE_X1, SLOPE_ZB),
                 (RAMP_X0, RAMP_H)], RIBN_Y0, RIB_Y0 + 0.01)
body = body.union(ramp)
# rib along the -Y side of the window, ending in a filler block at wall C
body = body.union(box(RIBN_X0, WC_X0 + 0.01, RIBN_Y0, RIBN_Y0 + RIBN_T, 0, RIB_H))
body = body.union(box(RIBN_X1, WC_X0 + 0.01, YI0 - 0.01, RIBN_Y0 + RIBN_T, 0, RIB_H))
body = body.union(box(RIB_X0, RIB_X1, RIB_Y0, RIB_Y0 + RIB_T, 0, RIB_H))

# concave fillet strip along the foot of the +Y wall
fil = (cq.Workplane("YZ")
       .moveTo(YI1 + 0.01, T_BASE - 0.01)
       .lineTo(YI1 + 0.01, T_BASE + WALL_FIL)
       .threePointArc((YI1 - WALL_FIL * 0.293, T_BASE + WALL_FIL * 0.293),
                      (YI1 - WALL_FIL, T_BASE - 0.01))
       .close()
       .extrude(WA_X0 - X_IN + 0.02).translate((X_IN - 0.01, 0, 0)))
body = body.union(fil)

# opening through the -X wall near the floor
body = body.cut(box(-0.1, X_IN + 0.1, OP_Y0, OP_Y1, OP_Z0, OP_Z1))

# ---------------- zig-zag inner wall at +X end ----------------
zz = box(WA_X0, BLK_X0, ZJ2_Y0, YI1 + 0.01, 0, H)                   # wall A
zz = zz.union(box(WB_X0, BLK_X0, ZJ2_Y0, ZJ2_Y1, 0, H))             # conn A-B
wall_b = (box(WB_X0, WB_X0 + ZW_T, ZJ1_Y0, ZJ2_Y1, 0, H)
          .edges("|Y and >X and >Z").fillet(WB_FIL))
zz = zz.union(wall_b)                                               # wall B
zz = zz.union(box(WB_X0, BLK_X0, ZJ1_Y0, ZJ1_Y1, 0, H))             # conn B-C
zz = zz.union(box(WC_X0, BLK_X0, YI0 - 0.01, ZJ1_Y1, 0, H))         # wall C
body = body.union(zz)

# ---------------- +X hinge blocks and channel ----------------
hinge = box(BLK_X0 - 0.01, L, YI0 - 0.01, YI1 + 0.01, 0, BLK_H)
hinge = hinge.cut(box(BLK_X0 - 0.1, LEDGE_X, YI0 - 0.1, YI1 + 0.1,
                      BLK_H - LEDGE_DROP, BLK_H + 1))
hinge = hinge.cut(box(LEDGE_X, L + 1, CH_Y0, CH_Y1, T_BASE, BLK_H + 1))
# small concave fillet between channel back wall and channel floor
ch_fil = (cq.Workplane("XZ")
          .moveTo(LEDGE_X - 0.01, T_BASE - 0.01)
          .lineTo(LEDGE_X + CH_FIL, T_BASE - 0.01)
          .threePointArc((LEDGE_X + CH_FIL * 0.293, T_BASE + CH_FIL * 0.293),
                         (LEDGE_X - 0.01, T_BASE + CH_FIL))
          .close()
          .extrude(-(CH_Y1 - CH_Y0)).translate((0, CH_Y0, 0)))
hinge = hinge.union(ch_fil)
body = body.union(hinge)

# hinge pin hole through everything along Y
pin = (cq.Workplane("XZ").center(PIN_X, PIN_Z).circle(PIN_D / 2)
       .extrude(-W - 2).translate((0, -1, 0)))
body = body.cut(pin)

# narrow through slot in the floor continuing the rib line
body = body.cut(box(SLOT_X0, SLOT_X1, SLOT_Y0, SLOT_Y0 + SLOT_W, -2, T_BASE + 0.5))

# window through the floor and pad
body = body.cut(box(WIN_X0, WIN_X1, WIN_Y0, WIN_Y1, -PAD_T - 1, T_BASE + 1))

# ---------------- tabs and posts near the +Y wall ----------------
for (x0, x1) in TABS:
    # tab standing on a floor patch so its foot can be filleted in isolation
    tab = box(x0, x1, TAB_Y0, TAB_Y0 + TAB_T, T_BASE - 0.5, TAB_H)
    patch = box(x0 - 2.0, x1 + 2.0, TAB_Y0 - 2.0, TAB_Y0 + TAB_T + 2.0,
                T_BASE - 0.5, T_BASE)
    tab = (patch.union(tab)
           .edges(cq.selectors.BoxSelector((x0 - 0.1, TAB_Y0 - 0.1, T_BASE - 0.1),
                                           (x1 + 0.1, TAB_Y0 + TAB_T + 0.1, T_BASE + 0.1)))
           .fillet(TAB_FIL))
    xc = 0.5 * (x0 + x1)
    holes = (cq.Workplane("XZ").pushPoints([(xc, TAB_HOLE_Z)])
             .circle(TAB_HOLE_D / 2)
             .extrude(-TAB_T - 2).translate((0, TAB_Y0 - 1, 0)))
    holes = holes.union(
        cq.Workplane("XZ")
        .pushPoints([(xc - TAB_PIN_DX, TAB_HOLE_Z), (xc + TAB_PIN_DX, TAB_HOLE_Z)])
        .circle(TAB_PIN_D / 2).extrude(-TAB_T - 2).translate((0, TAB_Y0 - 1, 0)))
    body = body.union(tab.cut(holes))

# posts: revolved profile with a concave fillet at the foot
r = POST_D / 2
post_prof = (cq.Workplane("XZ")
             .moveTo(0, T_BASE - 0.01)
             .lineTo(r + POST_FIL, T_BASE - 0.01)
             .threePointArc((r + POST_FIL * 0.293, T_BASE + POST_FIL * 0.293),
                            (r, T_BASE + POST_FIL))
             .lineTo(r, POST_H)
             .lineTo(0, POST_H)
             .close()
             .revolve(360, (0, 0, 0), (0, 1, 0)))
for i, (x, y) in enumerate(POSTS):
    body = body.union(post_prof.translate((x, y, 0)))
    # centre hole: blind from the top, except the middle post (through)
    z0 = -2.0 if i == POST_THROUGH else POST_H - 3.0
    body = body.cut(cq.Workplane("XY").center(x, y).circle(POST_HOLE / 2)
                    .extrude(POST_H + 1 - z0).translate((0, 0, z0)))

# small square holes in the floor
for (x, y) in SQ_HOLES:
    body = body.cut(box(x - 0.5, x + 0.5, y - 0.5, y + 0.5, -2, T_BASE + 1))

# small blind holes in the underside below the -Y wall
for (x, y) in BOT_HOLES:
    body = body.cut(cq.Workplane("XY").center(x, y).circle(BOT_HOLE_D / 2)
                    .extrude(BOT_HOLE_DEPTH + 1).translate((0, 0, -1)))

result = body
